import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------------------
# Driving dimensions (mm).  X = width, Y = length (front = -Y), Z = height
# ---------------------------------------------------------------------------
Y_FRONT_FACE = -84.35     # front face of the nose / roof
Y_STEP = -37.0            # step behind the raised nose
Y_MID = 52.0              # lowest point of the shoulder line
Y_TRANS = 59.0            # transverse wall (end of the under-cavity)
Y_BACK = 99.5             # back face of the rear block
Z_NOSE = 100.0            # top of the nose
Z_STEP = 88.0             # top just behind the nose step
Z_BACK = 44.0             # rear flat plate height
Y_KNEE, Z_KNEE = 28.0, 72.0   # end of the grooved slope behind the nose

PLATE_T = 12.4            # side plate thickness
X_OUT_FRONT_R = 87.2      # outer face of +X side plate at Y=-118
X_LUG_L = 92.8            # outer face |X| of the -X front lug
Y_JOG = -70.0             # -X side: lug ends / wall jogs outward here
X_JOG_L = 98.0            # |X| of -X wall outer face just behind the jog
X_OUT_BACK = 100.0        # outer face of side plates at Y=+118 (|X|)
NOSE_HW = 31.0            # nose half width at the front face
NOSE_HW_MID = 59.0        # shoulder top-corner half width at Y_MID

SH_Z_FRONT = 57.5         # shoulder / side-wall line heights
SH_Z_MID = 36.5
SH_Z_BACK = 44.0

T_ROOF = 10.0             # roof wall thickness
T_NOSE = 12.0
T_SH = 12.0               # shoulder wall thickness

RIB_X0, RIB_X1 = 18.7, 24.1   # internal vertical ribs (|X| range)
RIB_SETBACK = 2.0
RIB_FOOT_W = 12.0         # width of the tapered rib foot at Z=0
RIB_FOOT_H = 15.0

# front lug
LUG_C = (-93.5, 32.5)     # (Y, Z) centre of lug arc and pivot hole
LUG_R = 25.0
LUG_HOLE_D = 18.4
# rear knuckles
KN_C = (101.5, 17.0)      # (Y, Z) hinge axis
KN_R = 17.0
KN_PIN_D = 8.0
KN_MID_X = (-50.0, 0.0, 50.0)
KN_MID_W = 34.0
KN_OUT_W = 17.5
KN_BARREL_R = 15.0        # barrel radius between the end flanges
KN_TAB_T = 5.0            # end flange thickness


def x_out(y, s=1):
    """|X| of the outer face of the (splayed) side wall on side s at station y"""
    if s > 0:
        return X_OUT_FRONT_R + (y + 118.0) * (X_OUT_BACK - X_OUT_FRONT_R) / 236.0
    return X_JOG_L + (y - Y_JOG) * (X_OUT_BACK - X_JOG_L) / (118.0 - Y_JOG)


def xz_wire(pts, y):
    vs = [cq.Vector(x, y, z) for (x, z) in pts]
    return cq.Wire.makePolygon(vs, close=True)


def line_intersect(p1, d1, p2, d2):
    den = d1[0] * d2[1] - d1[1] * d2[0]
    t = ((p2[0] - p1[0]) * d2[1] - (p2[1] - p1[1]) * d2[0]) / den
    return (p1[0] + t * d1[0], p1[1] + t * d1[1])


def offset_poly(pts, offs):
    """inward offset of a CCW convex polygon, per-edge offsets"""
    n = len(pts)
    lines = []
    for i in range(n):
        a, b = pts[i], pts[(i + 1) % n]
        d = (b[0] - a[0], b[1] - a[1])
        ln = math.hypot(*d)
        nin = (-d[1] / ln, d[0] / ln)          # inward normal for CCW
        o = offs[i]
        lines.append(((a[0] + nin[0] * o, a[1] + nin[1] * o), d))
    out = []
    for i in range(n):
        p1, d1 = lines[i - 1]
        p2, d2 = lines[i]
        out.append(line_intersect(p1, d1, p2, d2))
    return out


def roof_section(y, sh_z, top_hw):
    xr, xl = x_out(y, 1), x_out(y, -1)
    return [(-xl, 0.0), (xr, 0.0), (xr, sh_z), (top_hw, Z_NOSE),
            (-top_hw, Z_NOSE), (-xl, sh_z)]


def lerp(a, b, t):
    return a + (b - a) * t


# ---------------------------------------------------------------------------
# outer roof body: ruled loft through three hexagonal stations
# ---------------------------------------------------------------------------
# top corner of the shoulder lines at Z=Z_NOSE
def top_hw(y):
    t = (y - Y_FRONT_FACE) / (Y_MID - Y_FRONT_FACE)
    return lerp(NOSE_HW, NOSE_HW_MID, t)


S_front = roof_section(Y_FRONT_FACE, SH_Z_FRONT, top_hw(Y_FRONT_FACE))
S_mid = roof_section(Y_MID, SH_Z_MID, top_hw(Y_MID))
S_back = [(-x_out(Y_BACK, -1), 0.0), (x_out(Y_BACK, 1), 0.0),
          (x_out(Y_BACK, 1), SH_Z_BACK), (72.0, Z_NOSE), (-72.0, Z_NOSE),
          (-x_out(Y_BACK, -1), SH_Z_BACK)]

roof_outer = cq.Solid.makeLoft(
    [xz_wire(S_front, Y_FRONT_FACE), xz_wire(S_mid, Y_MID),
     xz_wire(S_back, Y_BACK)], True)

# side (YZ) profile trimming the top
top_prof = [(Y_FRONT_FACE, -20), (Y_FRONT_FACE, Z_NOSE), (Y_STEP, Z_NOSE),
            (Y_STEP, Z_STEP), (Y_KNEE, Z_KNEE), (57.0, 52.5), (66.0, 48.0),
            (Y_BACK, Z_BACK), (Y_BACK, -20)]
top_cut = (cq.Workplane("YZ").workplane(offset=-200).polyline(top_prof).close()
           .extrude(400))

body = cq.Workplane().add(roof_outer).intersect(top_cut)


# ---------------------------------------------------------------------------
# under cavity (open bottom + front)
# ---------------------------------------------------------------------------
offs = [-15.0, PLATE_T, T_SH, T_ROOF, T_SH, PLATE_T]


def inner_section(y):
    if y <= Y_MID:
        t = (y - Y_FRONT_FACE) / (Y_MID - Y_FRONT_FACE)
        pts = [(lerp(a[0], b[0], t), lerp(a[1], b[1], t)) for a, b in zip(S_front, S_mid)]
    else:
        t = (y - Y_MID) / (Y_BACK - Y_MID)
        pts = [(lerp(a[0], b[0], t), lerp(a[1], b[1], t)) for a, b in zip(S_mid, S_back)]
    return offset_poly(pts, offs)


Y_CAV0 = -110.0
cav = cq.Solid.makeLoft(
    [xz_wire(inner_section(Y_CAV0), Y_CAV0), xz_wire(inner_section(Y_MID), Y_MID),
     xz_wire(inner_section(Y_TRANS), Y_TRANS)], True)
in_prof = [(Y_CAV0, -30), (Y_CAV0, Z_NOSE - T_NOSE), (Y_STEP - 8.0, Z_NOSE - T_NOSE),
           (Y_STEP, Z_STEP - T_ROOF), (Y_KNEE, Z_KNEE - T_ROOF), (Y_TRANS, 20.0),
           (Y_TRANS, -30)]
in_cut = (cq.Workplane("YZ").workplane(offset=-200).polyline(in_prof).close()
          .extrude(400))
cavity = cq.Workplane().add(cav).intersect(in_cut)

body_outer = body
body = body.cut(cavity)

# internal vertical ribs
for s in (-1, 1):
    rib = (cq.Workplane("XY")
           .center(s * (RIB_X0 + RIB_X1) / 2, (Y_FRONT_FACE + RIB_SETBACK + Y_TRANS) / 2)
           .rect(RIB_X1 - RIB_X0, Y_TRANS - Y_FRONT_FACE - RIB_SETBACK).extrude(110))
    body = body.union(rib.intersect(body_outer))
    # tapered foot along the bottom of each rib
    xc = s * (RIB_X0 + RIB_X1) / 2
    hw0, hw1 = RIB_FOOT_W / 2, (RIB_X1 - RIB_X0) / 2
    foot = (cq.Workplane("XZ").workplane(offset=-(Y_FRONT_FACE + RIB_SETBACK))
            .polyline([(xc - hw0, 0.0), (xc + hw0, 0.0), (xc + hw1, RIB_FOOT_H),
                       (xc - hw1, RIB_FOOT_H)]).close()
            .extrude(-(Y_TRANS - Y_FRONT_FACE - RIB_SETBACK)))
    body = body.union(foot)

# raked front edge of the shoulders (opens the front corners)
for s in (-1, 1):
    rake = (cq.Workplane("XY")
            .polyline([(s * 34.0, Y_FRONT_FACE - 1.0), (s * 34.0, Y_FRONT_FACE),
                       (s * 92.0, -71.0), (s * 140.0, -71.0), (s * 140.0, -140.0),
                       (s * 34.0, -140.0)]).close()
            .extrude(120).translate((0, 0, 56.0)))
    body = body.cut(rake)

# ---------------------------------------------------------------------------
# side plates
# ---------------------------------------------------------------------------
def tangent_point(p, c, r, side):
    dx, dy = p[0] - c[0], p[1] - c[1]
    d = math.hypot(dx, dy)
    a = math.atan2(dy, dx)
    b = math.acos(r / d)
    ang = a + side * b
    return (c[0] + r * math.cos(ang), c[1] + r * math.sin(ang))


def plate_profile():
    cy, cz = LUG_C
    p0 = (-92.0, 0.0)
    tp = tangent_point(p0, LUG_C, LUG_R, -1)
    mid = (cy - LUG_R, cz)
    top = (cy, cz + LUG_R)
    ky, kz = KN_C
    wp = (cq.Workplane("YZ")
          .moveTo(*p0).lineTo(*tp)
          .threePointArc(mid, top)
          .lineTo(Y_FRONT_FACE, SH_Z_FRONT)
          .lineTo(Y_MID, SH_Z_MID)
          .lineTo(Y_BACK, SH_Z_BACK)
          .lineTo(Y_BACK, kz + KN_R)
          .lineTo(ky, kz + KN_R)
          .threePointArc((ky + KN_R, kz), (ky, kz - KN_R))
          .close())
    return wp


def side_plate_r():
    splay = math.atan2(X_OUT_BACK - X_OUT_FRONT_R, 236.0)
    pl = plate_profile().extrude(PLATE_T).translate((-PLATE_T, 0, 0))
    # rotate for splay (back end outward) and move onto the outer face line
    pl = pl.rotate((0, 0, 0), (0, 0, 1), -math.degrees(splay))
    return pl.translate((x_out(0.0, 1), 0, 0))


def side_wall_l():
    """-X side: straight front lug, wall jogged outward behind it"""
    front_box = cq.Workplane("XY").box(400, 200, 400, centered=(True, False, True)) \
        .translate((0, Y_JOG - 200.0, 0))
    lug = (plate_profile().extrude(PLATE_T).translate((-X_LUG_L, 0, 0))
           .intersect(front_box))
    splay = math.atan2(X_OUT_BACK - X_JOG_L, 118.0 - Y_JOG)
    rear = plate_profile().extrude(PLATE_T)
    rear = rear.rotate((0, 0, 0), (0, 0, 1), math.degrees(splay))
    rear = rear.translate((-(X_JOG_L - Y_JOG * math.tan(splay)), 0, 0))
    rear = rear.cut(front_box)
    return lug, rear


plate_r = side_plate_r()
lug_l, wall_l = side_wall_l()
body = body.union(plate_r).union(wall_l)

# trim the roof side wall in front of the jog on the -X side (outside the lug)
trim = (cq.Workplane("XY").box(60, 80, 68, centered=(False, False, False))
        .translate((-X_LUG_L - 60.0, Y_JOG - 80.0, -1.0)))
body = body.cut(trim)

# arch opening in the -X side wall
arch = (cq.Workplane("YZ").workplane(offset=-130)
        .moveTo(Y_JOG, -10.0).lineTo(Y_JOG, 40.0)
        .threePointArc((-45.0, 46.5), (-6.0, 44.5))
        .threePointArc((16.0, 30.0), (32.0, 0.0))
        .lineTo(32.0, -10.0).close()
        .extrude(130.0 - 72.0))
body = body.cut(arch)
body = body.union(lug_l)

# bent web ("C" flange) behind the -X lug, turned inward at 45 deg
FL_U = cq.Vector(math.sqrt(0.5), math.sqrt(0.5), 0)
FL_N = cq.Vector(math.sqrt(0.5), -math.sqrt(0.5), 0)
FL_T = 6.0
FL_BULGE = 10.0
fl_org = cq.Vector(-X_LUG_L + PLATE_T, Y_JOG, 0) - FL_N * (FL_T / 2)
fl_pl = cq.Plane(origin=fl_org, xDir=FL_U, normal=FL_N)
flange = (cq.Workplane(fl_pl).moveTo(-4.0, 0.5).lineTo(-4.0, 56.0).lineTo(0.0, 56.0)
          .threePointArc((FL_BULGE, 29.0), (0.0, 0.5)).close()
          .extrude(FL_T / 2, both=True))
body = body.union(flange)

# ---------------------------------------------------------------------------
# rear hinge knuckles
# ---------------------------------------------------------------------------
ky, kz = KN_C


def knuckle(xc, w):
    k = (cq.Workplane("YZ").workplane(offset=xc - w / 2)
         .moveTo(80.0, kz - KN_R).lineTo(ky, kz - KN_R)
         .threePointArc((ky + KN_R, kz), (ky, kz + KN_R))
         .lineTo(80.0, kz + KN_R).close()
         .extrude(w))
    return k


def hinge_tab(x0, t):
    """end flange of a middle knuckle: round end with a faceted top"""
    c = (cq.Workplane("YZ").workplane(offset=x0).center(ky, kz)
         .circle(KN_R).extrude(t))
    p = (cq.Workplane("YZ").workplane(offset=x0)
         .polyline([(84.0, kz), (84.0, kz + KN_R + 3.0), (ky - 3.0, kz + KN_R + 3.0),
                    (ky + 11.0, kz + 10.0), (ky, kz)]).close().extrude(t))
    return c.union(p)


def mid_knuckle(xc, w):
    barrel = (cq.Workplane("YZ").workplane(offset=xc - w / 2)
              .moveTo(84.0, kz - KN_BARREL_R).lineTo(ky, kz - KN_BARREL_R)
              .threePointArc((ky + KN_BARREL_R, kz), (ky, kz + KN_BARREL_R))
              .lineTo(84.0, kz + KN_BARREL_R).close()
              .extrude(w))
    barrel = barrel.union(hinge_tab(xc - w / 2, KN_TAB_T))
    barrel = barrel.union(hinge_tab(xc + w / 2 - KN_TAB_T, KN_TAB_T))
    return barrel


for xc in KN_MID_X:
    body = body.union(mid_knuckle(xc, KN_MID_W))
for s in (-1, 1):
    xin = x_out(ky, s) - KN_OUT_W
    xc = s * (xin + (KN_OUT_W - 3.0) / 2)
    body = body.union(knuckle(xc, KN_OUT_W - 3.0))

# notches in the rear block between knuckles
gaps = [(-74.5, 16.0), (-25.0, 16.0), (25.0, 16.0), (74.5, 16.0)]
for gx, gw in gaps:
    notch = (cq.Workplane("XY").center(gx, 100.0).rect(gw, 36.0)
             .extrude(kz + KN_R + 1.0).translate((0, 0, -1.0)))
    body = body.cut(notch)

# pin bore through middle knuckles
pin = (cq.Workplane("YZ").workplane(offset=-80).center(ky, kz)
       .circle(KN_PIN_D / 2).extrude(160))
body = body.cut(pin)

# slots in the outer knuckles (side plate rear ends)
for s_ in (-1, 1):
    slot = (cq.Workplane("YZ").workplane(offset=s_ * 90.0 - 20.0).center(ky - 3.0, kz)
            .slot2D(10.5, 7.5).extrude(40))
    body = body.cut(slot)
for s in (-1, 1):
    cb = (cq.Workplane("YZ").workplane(offset=s * x_out(ky, s) - 2.0).center(ky - 3.0, kz)
          .slot2D(16.0, 11.5).extrude(4.0))
    body = body.cut(cb)

# front lug pivot holes
for s_ in (-1, 1):
    lug_hole = (cq.Workplane("YZ").workplane(offset=s_ * 85.0 - 20.0).center(*LUG_C)
                .circle(LUG_HOLE_D / 2).extrude(40))
    body = body.cut(lug_hole)

# ---------------------------------------------------------------------------
# small features on top
# ---------------------------------------------------------------------------
# four holes in rear flat plate
for x, y in ((-69.0, 67.5), (-24.0, 74.0), (24.0, 74.0), (69.0, 67.5)):
    h = (cq.Workplane("XY").workplane(offset=Z_BACK - 20).center(x, y)
         .slot2D(11.5, 8.8, angle=90).extrude(35))
    body = body.cut(h)

# four holes in the nose front face
for x in (-18.3, -6.1, 6.1, 18.3):
    h = (cq.Workplane("XZ").workplane(offset=-Y_FRONT_FACE + 1.0).center(x, 94.0)
         .circle(4.0).extrude(-28.0))
    body = body.cut(h)

# keyholes on the nose top
for x in (-21.25, -5.0, 11.5, 28.75):
    h = cq.Workplane("XY").workplane(offset=Z_NOSE - 15).center(x, -57.5).circle(3.0).extrude(20)
    sl = (cq.Workplane("XY").workplane(offset=Z_NOSE - 15)
          .polyline([(x - 1.4, -57.5), (x + 1.4, -57.5), (x + 0.4, -43.0), (x - 0.4, -43.0)])
          .close().extrude(20))
    body = body.cut(h).cut(sl)

# small holes on the shoulders
for s in (-1, 1):
    h = cq.Workplane("XY").workplane(offset=50).center(s * 72.0, -40.0).circle(2.0).extrude(40)
    body = body.cut(h)

# sloped top plane (behind the nose step) for grooves and kite pocket
p_a = cq.Vector(0, Y_STEP, Z_STEP)
p_b = cq.Vector(0, Y_KNEE, Z_KNEE)
slope_dir = (p_b - p_a).normalized()
top_normal = cq.Vector(0, -slope_dir.z, slope_dir.y).normalized()
if top_normal.z < 0:
    top_normal = -top_normal


def on_top(x, y):
    z = Z_STEP + (y - Y_STEP) * (Z_KNEE - Z_STEP) / (Y_KNEE - Y_STEP)
    return cq.Vector(x, y, z)


groove_keep = cq.Workplane("XY").box(300, 300, 300, centered=(True, False, True)).translate((0, Y_STEP, 0))


def groove(p0, p1, w, depth):
    """groove normal to the sloped top, open towards the nose step"""
    a = on_top(*p0)
    b = on_top(*p1)
    d = (b - a)
    ln = d.Length
    pl = cq.Plane(origin=a, xDir=d.normalized(), normal=top_normal)
    g = (cq.Workplane(pl).workplane(offset=-depth).center(ln / 2, 0).rect(ln, w)
         .extrude(depth + 10))
    g = g.union(cq.Workplane(pl).workplane(offset=-depth).center(ln, 0).circle(w / 2)
                .extrude(depth + 10))
    return g.intersect(groove_keep)


GROOVES = (((-26.0, -45.0), (-38.6, 11.0)), ((-12.0, -45.0), (-19.1, 32.0)),
           ((14.2, -45.0), (21.0, 32.0)), ((34.0, -45.0), (49.5, 9.5)))
for p0, p1 in GROOVES:
    body = body.cut(groove(p0, p1, 8.0, 5.0))

# kite-shaped pocket with a through hole
kite = [(2.0, 34.8), (-12.7, 21.0), (5.2, -2.3), (16.9, 22.0)]
kpl = cq.Plane(origin=on_top(0, 0), xDir=cq.Vector(1, 0, 0), normal=top_normal)
kite_local = []
for x, y in kite:
    v = on_top(x, y) - on_top(0, 0)
    kite_local.append((v.dot(kpl.xDir), v.dot(kpl.yDir)))
kp = (cq.Workplane(kpl).workplane(offset=-4.0).polyline(kite_local).close()
      .extrude(15))
body = body.cut(kp)
kh = cq.Workplane("XY").center(2.7, 23.8).circle(3.0).extrude(120)
body = body.cut(kh)


# small fixing holes in the bottom face of the +X side plate
for y in (-59.0, -43.5, -27.0, 6.0, 25.5, 46.0, 67.0):
    xm = x_out(y, 1) - PLATE_T / 2
    h = cq.Workplane("XY").workplane(offset=-1.0).center(xm, y).circle(1.8).extrude(11)
    body = body.cut(h)

# fixing holes in the rear bottom strip and -X side
for x, y in ((-58.25, 77.5), (-41.75, 77.5), (-8.25, 77.5), (8.25, 77.5),
             (41.75, 77.5), (58.25, 77.5), (-92.0, 66.0), (-92.0, 45.0),
             (-86.6, -80.0), (-86.6, -73.5)):
    h = cq.Workplane("XY").workplane(offset=-1.0).center(x, y).circle(1.8).extrude(11)
    body = body.cut(h)

result = body
